import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
SPAN = 30.0            # overall width of the cross-shaped head (X and Y)
ARM_W = SPAN / 3.0     # width of each cross arm
HUB_R = SPAN / 3.0     # radius of the central round hub of the head
HEAD_H = 10.0          # head thickness

THREAD_MAJOR = 14.2    # thread crest diameter
THREAD_ROOT = 12.85    # thread root / core diameter
SHANK_LEN = 12.5       # length of the shank below the head (to the tip)
PITCH = 1.57           # thread pitch (right hand)
THREAD_TURNS = 7.40    # number of helical turns of the thread
THREAD_END_DEPTH = 12.14   # depth below head of the lower thread end (tooth centre)
THREAD_END_ANGLE = 273.0   # azimuth (deg, CCW from +X) of the lower thread end
RUNOUT = 60.0          # angular length (deg) over which the tooth fades in / out
ROOT_W = 1.05          # axial width of thread tooth at the root
CREST_W = 0.75         # axial width of the flat crest

TAPER_LEN = 5.0        # conical tip length
TAPER_TOP_D = 12.4     # tip diameter where it joins the shank
TAPER_BOT_D = 9.9      # tip end diameter
SEAM_ANGLE = 90.0      # azimuth where round faces put their seam (kept out of view)

# ---------------- head: cross + round hub ----------------
head = (
    cq.Workplane("XY")
    .rect(SPAN, ARM_W).extrude(HEAD_H)
    .union(cq.Workplane("XY").rect(ARM_W, SPAN).extrude(HEAD_H))
    .union(cq.Workplane("XY").circle(HUB_R).extrude(HEAD_H))
)

# ---------------- shank core ----------------
r_root = THREAD_ROOT / 2
r_maj = THREAD_MAJOR / 2
core = (
    cq.Workplane("XY").circle(r_root).extrude(-SHANK_LEN)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

# ---------------- helical thread with run-outs ----------------
r_in = r_root - 0.05                 # tooth base sits slightly inside the core
FULL = r_maj - r_in                  # full radial tooth height
END_SCALE = 0.04                     # tooth scale at the very ends (buried in the core)


def tooth(scale, ang, anchor=0.0):
    """Trapezoid tooth section scaled by `scale` about the root point at axial
    offset `anchor` (so a run-out tooth shrinks toward one crest edge),
    placed on the helix at `ang` deg."""
    za = anchor * (1.0 - scale)
    w = (
        cq.Workplane("XZ")
        .polyline([
            (r_in, za - scale * ROOT_W / 2),
            (r_in + scale * FULL, za - scale * CREST_W / 2),
            (r_in + scale * FULL, za + scale * CREST_W / 2),
            (r_in, za + scale * ROOT_W / 2),
        ])
        .close()
        .wire()
        .val()
    )
    return place(w, ang)


def place(shape, ang):
    """Rotate about Z by `ang` deg and lift by the matching helix rise."""
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ang).translate(
        cq.Vector(0, 0, PITCH * ang / 360.0)
    )


total = THREAD_TURNS * 360.0
run_helix = cq.Wire.makeHelix(pitch=PITCH, height=PITCH * RUNOUT / 360.0, radius=r_in)
main_helix = cq.Wire.makeHelix(
    pitch=PITCH, height=PITCH * (total - 2 * RUNOUT) / 360.0, radius=r_in
)
lead_in = cq.Solid.sweep_multi(
    [tooth(END_SCALE, 0, CREST_W / 2), tooth(1.0, RUNOUT)], run_helix, makeSolid=True, isFrenet=True
)
body = place(cq.Solid.sweep(tooth(1.0, 0), [], main_helix, isFrenet=True), RUNOUT)
lead_out = place(
    cq.Solid.sweep_multi(
        [tooth(1.0, 0), tooth(END_SCALE, RUNOUT, -CREST_W / 2)], run_helix, makeSolid=True, isFrenet=True
    ),
    total - RUNOUT,
)
thread = (
    cq.Workplane("XY").add(body)
    .union(cq.Workplane("XY").add(lead_in))
    .union(cq.Workplane("XY").add(lead_out))
    .rotate((0, 0, 0), (0, 0, 1), THREAD_END_ANGLE)
    .translate((0, 0, -THREAD_END_DEPTH))
)
# nothing of the thread may hang below the shank (tip joins there)
shank_zone = (
    cq.Workplane("XY", origin=(0, 0, -SHANK_LEN))
    .circle(r_maj + 1.0)
    .extrude(SHANK_LEN)
)
thread = thread.intersect(shank_zone)

# ---------------- conical tip ----------------
tip = (
    cq.Workplane("XZ")
    .polyline([
        (0, -SHANK_LEN),
        (TAPER_TOP_D / 2, -SHANK_LEN),
        (TAPER_BOT_D / 2, -SHANK_LEN - TAPER_LEN),
        (0, -SHANK_LEN - TAPER_LEN),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

result = head.union(core).union(thread).union(tip)

VIEW = {"azimuth": 45, "elevation": 26}
